import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R_FLANGE = 60.0        # outer radius of the top plate / flange
T_TOP = 3.3            # thickness of the perforated top plate
R_SKIRT = 51.6         # outer radius of the skirt (spigot) below the flange
H_SKIRT = 17.3         # skirt height below the flange
W_SKIRT = 3.2          # outer skirt wall thickness
GROOVE_W = 3.7         # annular groove between outer skirt and inner ring
W_RING = 1.7           # inner ring wall thickness
RING_LIFT = 1.3        # inner ring stops this far above the skirt bottom
ROUND_A = 3.0          # elliptical round on the flange top edge: radial size
ROUND_B = 2.0          # elliptical round on the flange top edge: axial size
SEAM_ANGLE = 96.0      # where the revolve seams sit (hidden side, between words)

D_BIG = 8.4            # large vent holes (centre, inner and middle rings)
D_OUTER = 7.8          # large vent holes of the outer ring
D_SMALL = 2.7          # small vent holes

# hole rings: (radius, count, start angle deg, diameter)
HOLE_RINGS = [
    (0.0, 1, 0.0, D_BIG),        # centre hole
    (12.0, 5, 63.0, D_BIG),      # inner ring of large holes
    (15.5, 5, 24.5, D_SMALL),    # inner ring of small holes
    (25.1, 10, 2.0, D_BIG),      # middle ring of large holes
    (28.2, 10, 19.5, D_SMALL),   # middle ring of small holes
    (36.8, 16, 11.25, D_OUTER),  # outer ring of large holes
]

# engraved lettering around the rim
TEXT_SIZE = 7.2
TEXT_DEPTH = 0.6
TEXT_BASE_R = 51.2
TEXT_FONT = "DejaVu Sans"
WORDS = [("Smoky", 80.0 - 60.0 * k) for k in range(6)] + \
        [("Tuch", 110.0 - 60.0 * k) for k in range(6)]

# mounting bosses inside the skirt
BOSS_ANGLES = [45.0, 135.0, 225.0, 315.0]
BOSS_C_R = 39.0        # inner lobe centre radius
BOSS_C_D = 6.8
BOSS_B_R = 44.9        # outer lobe centre radius (runs into the wall)
BOSS_B_D = 5.8
HOLE_A_R = 48.7        # small hole in the wall itself
PIN_D = 1.0            # pilot hole diameter

H_TOTAL = H_SKIRT + T_TOP
Z_TOP = H_TOTAL

# ---------------- body ----------------
# flange / top plate as a revolved profile with a soft elliptical top edge
flange = (cq.Workplane("XZ")
          .moveTo(0.0, H_SKIRT)
          .lineTo(R_FLANGE, H_SKIRT)
          .lineTo(R_FLANGE, Z_TOP - ROUND_B)
          .ellipseArc(ROUND_A, ROUND_B, 0.0, 90.0, startAtCurrent=True)
          .lineTo(0.0, Z_TOP)
          .close()
          .revolve(360.0, (0, 0, 0), (0, 1, 0)))

R_OUT_IN = R_SKIRT - W_SKIRT          # inner face of the outer skirt
R_RING_O = R_OUT_IN - GROOVE_W        # outer face of the inner ring
R_RING_I = R_RING_O - W_RING          # inner face of the inner ring


def ring(r_in, r_out, z0, z1):
    prof = [(r_in, z0), (r_out, z0), (r_out, z1), (r_in, z1)]
    return (cq.Workplane("XZ").polyline(prof).close()
            .revolve(360.0, (0, 0, 0), (0, 1, 0)))


skirt = ring(R_OUT_IN, R_SKIRT, 0.0, H_SKIRT + 0.01)
inner_ring = ring(R_RING_I, R_RING_O, RING_LIFT, H_SKIRT + 0.01)
# turn the periodic seams of the revolved faces to the back of the part
flange = flange.rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE)
skirt = skirt.rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE)
inner_ring = inner_ring.rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE)
body = flange.union(skirt).union(inner_ring)

# bosses: a round inner lobe on the inner ring plus an obround outer lobe
# that bridges the groove into the outer skirt, full skirt height
for a in BOSS_ANGLES:
    ar = math.radians(a)
    cyl = (cq.Workplane("XY")
           .center(BOSS_C_R * math.cos(ar), BOSS_C_R * math.sin(ar))
           .circle(BOSS_C_D / 2.0).extrude(H_SKIRT + 0.01))
    body = body.union(cyl)
    r0 = BOSS_B_R - BOSS_B_D / 2.0
    r1 = R_SKIRT - 0.4
    rc = 0.5 * (r0 + r1)
    lobe = (cq.Workplane("XY")
            .center(rc * math.cos(ar), rc * math.sin(ar))
            .slot2D(r1 - r0, BOSS_B_D, a).extrude(H_SKIRT + 0.01))
    body = body.union(lobe)

# pilot holes in bosses and wall (blind, from the bottom)
pin_pts = []
for a in BOSS_ANGLES:
    ar = math.radians(a)
    for r in (BOSS_C_R, BOSS_B_R, HOLE_A_R):
        pin_pts.append((r * math.cos(ar), r * math.sin(ar)))
pins = (cq.Workplane("XY").pushPoints(pin_pts).circle(PIN_D / 2.0)
        .extrude(H_SKIRT - 2.0))
body = body.cut(pins)

# vent holes through the top plate
pts_by_d = {}
for (r, n, a0, d) in HOLE_RINGS:
    for i in range(n):
        a = math.radians(a0 + 360.0 * i / n)
        pts_by_d.setdefault(d, []).append((r * math.cos(a), r * math.sin(a)))
for d, pts in pts_by_d.items():
    cutter = (cq.Workplane("XY").workplane(offset=H_SKIRT - 1.0)
              .pushPoints(pts).circle(d / 2.0).extrude(T_TOP + 2.0))
    body = body.cut(cutter)

# ---------------- lettering on an arc ----------------
letters = []
r_arc = TEXT_BASE_R + 0.35 * TEXT_SIZE
for word, ang in WORDS:
    txt = cq.Workplane("XY").text(word, TEXT_SIZE, TEXT_DEPTH + 1.0,
                                  halign="center", valign="bottom",
                                  font=TEXT_FONT, kind="regular",
                                  combine=False)
    for comp in txt.vals():
        for s in comp.Solids():
            bb = s.BoundingBox()
            cx = 0.5 * (bb.xmin + bb.xmax)
            s1 = s.translate(cq.Vector(-cx, TEXT_BASE_R, Z_TOP - TEXT_DEPTH))
            rot = ang - 90.0 - math.degrees(cx / r_arc)
            s2 = s1.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), rot)
            letters.append(s2)

if letters:
    body = body.cut(cq.Workplane("XY").add(cq.Compound.makeCompound(letters)))

result = body

VIEW = {"azimuth": 45, "elevation": 26}
